import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 54.0            # outer footprint (square)
R_OUT = 6.8         # outer corner radius
H = 8.9             # rim (outer lip) height
T_WALL = 2.5        # total wall thickness
T_LIP = 1.05        # thickness of the raised outer lip
Z_LEDGE = 7.4       # height of the inner ledge / corner bosses
FLOOR_T = 1.55      # floor thickness
Z_SLOT_FENCE = 5.1  # top of the fence around the long slot
Z_FENCE = 5.0       # top of the other fences
T_FENCE = 1.1       # fence wall thickness
R_IN = 0.9          # corner radius of the openings (convex corners)
Z_PIN = 10.7        # top of locating pins
Z_NOTCH = 2.3       # bottom of the notches in the -X wall
Z_BOSS = 6.65       # top of the round boss

CORNER_BOSS = 19.7  # corner bosses occupy |x|,|y| >= this
CORNER_HOLE_D = 1.8
CORNER_HOLE_C = 22.1
CORNER_HOLE_DEPTH = 4.0

HALF = W / 2.0
IN_HALF = HALF - T_WALL

# notches in the -X wall: (y_min, y_max)
NOTCHES = [(9.74, 17.34), (-12.93, -3.5)]

# ---- openings: interior outlines (x, y, corner radius) ----
SLOT = [
    (-6.17, 13.38, R_IN), (22.53, 13.38, R_IN),
    (22.53, 18.82, R_IN), (-6.17, 18.82, R_IN),
]
T_OPEN = [
    (-14.80, -18.95, 2.4), (22.68, -18.95, R_IN), (22.68, -13.56, R_IN),
    (-3.70, -13.56, 0.0), (-3.70, -3.85, R_IN), (-7.24, -3.85, R_IN),
    (-7.24, -11.32, 0.0), (-14.80, -11.32, R_IN),
]
RECT_A = [
    (19.23, -4.49, R_IN * 0.8), (24.33, -4.49, R_IN * 0.8),
    (24.33, 2.55, R_IN * 0.8), (19.23, 2.55, R_IN * 0.8),
]
RECT_B = [
    (16.42, -8.71, R_IN * 0.8), (19.94, -8.71, R_IN * 0.8),
    (19.94, -5.20, R_IN * 0.8), (16.42, -5.20, R_IN * 0.8),
]

# pins: (x, y, d)
PIN_D = 4.0
PINS = [
    (-14.30, 17.08, 3.3),
    (IN_HALF - PIN_D / 2 + 0.15, 13.3, PIN_D),
    (IN_HALF - PIN_D / 2 + 0.15, -6.3, PIN_D),
]

# post in the (-X,-Y) corner of the T opening: round body with a flat
# +X face and a flat +Y face, blended into the fence wall by a concave cove
POST_C = (-13.97, -17.47)
POST_R = 1.63
POST_FLAT_X = -12.6
POST_FLAT_Y = -16.75
POST_TAB = (-15.5, -14.0, -16.8, -15.96)   # x0, x1, y0, y1 of the blend block
POST_COVE_C = (-14.05, -15.9)
POST_COVE_R = 0.95

# boss with through hole near the (-X,-Y) corner
BOSS_C = (-20.0, -16.7)
BOSS_D = 5.5
BOSS_HOLE_D = 3.2
BOSS_CSK_D = 4.8


def rounded_outline(pts, offset=0.0, z=0.0):
    """Closed wire through axis-aligned polygon corners (x, y, r).

    Each corner is rounded with radius r (0 = sharp).  With offset > 0
    the outline is grown outward by `offset` (convex corner radii grow,
    concave corner radii shrink)."""
    n = len(pts)
    # signed area -> orientation
    area = 0.0
    for i in range(n):
        x0, y0, _ = pts[i]
        x1, y1, _ = pts[(i + 1) % n]
        area += x0 * y1 - x1 * y0
    ccw = area > 0

    # offset the polygon edges (axis aligned) outward
    corners = []
    for i in range(n):
        px, py, pr = pts[i - 1]
        cx, cy, cr = pts[i]
        nx_, ny_, nr = pts[(i + 1) % n]
        d_in = (cx - px, cy - py)
        d_out = (nx_ - cx, ny_ - cy)

        def outward(d):
            l = math.hypot(*d)
            ux, uy = d[0] / l, d[1] / l
            # right-hand normal is outward for ccw polygons
            return (uy, -ux) if ccw else (-uy, ux)

        n1 = outward(d_in)
        n2 = outward(d_out)
        ox = cx + offset * (n1[0] + n2[0])
        oy = cy + offset * (n1[1] + n2[1])
        cross = d_in[0] * d_out[1] - d_in[1] * d_out[0]
        convex = (cross > 0) == ccw
        if cr > 0:
            r = cr + offset if convex else cr - offset
        else:
            r = 0.0
        corners.append((ox, oy, max(r, 0.0)))

    # build wire with tangent arcs
    segs = []
    for i in range(n):
        px, py, _ = corners[i - 1]
        cx, cy, r = corners[i]
        nx_, ny_, _ = corners[(i + 1) % n]
        if r <= 1e-6:
            segs.append(("pt", (cx, cy)))
            continue
        u1 = (px - cx, py - cy)
        l1 = math.hypot(*u1)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (nx_ - cx, ny_ - cy)
        l2 = math.hypot(*u2)
        u2 = (u2[0] / l2, u2[1] / l2)
        t1 = (cx + u1[0] * r, cy + u1[1] * r)
        t2 = (cx + u2[0] * r, cy + u2[1] * r)
        b = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*b)
        b = (b[0] / lb, b[1] / lb)
        ctr = (cx + b[0] * r * math.sqrt(2), cy + b[1] * r * math.sqrt(2))
        mid = (ctr[0] - b[0] * r, ctr[1] - b[1] * r)
        segs.append(("arc", t1, mid, t2))

    edges = []
    # start point of each segment / end point
    def seg_start(s):
        return s[1] if s[0] == "pt" else s[1]

    def seg_end(s):
        return s[1] if s[0] == "pt" else s[3]

    for i, s in enumerate(segs):
        if s[0] == "arc":
            edges.append(
                cq.Edge.makeThreePointArc(
                    cq.Vector(s[1][0], s[1][1], z),
                    cq.Vector(s[2][0], s[2][1], z),
                    cq.Vector(s[3][0], s[3][1], z),
                )
            )
        e0 = seg_end(s)
        e1 = seg_start(segs[(i + 1) % len(segs)])
        if math.hypot(e1[0] - e0[0], e1[1] - e0[1]) > 1e-6:
            edges.append(
                cq.Edge.makeLine(cq.Vector(e0[0], e0[1], z), cq.Vector(e1[0], e1[1], z))
            )
    return cq.Wire.assembleEdges(edges)


def prism(pts, z0, z1, offset=0.0):
    wire = rounded_outline(pts, offset=offset, z=z0)
    face = cq.Face.makeFromWires(wire)
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0))
    return cq.Workplane("XY").add(solid)


# ---------------- outer shell ----------------
body = (
    cq.Workplane("XY")
    .rect(W, W)
    .extrude(H)
    .edges("|Z")
    .fillet(R_OUT)
)

# step on the top of the wall: keep only a thin outer lip above the ledge
lip_cut = (
    cq.Workplane("XY")
    .workplane(offset=Z_LEDGE)
    .rect(W - 2 * T_LIP, W - 2 * T_LIP)
    .extrude(H)
    .edges("|Z")
    .fillet(R_OUT - T_LIP)
)
body = body.cut(lip_cut)

# main cavity
cavity = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_T)
    .rect(2 * IN_HALF, 2 * IN_HALF)
    .extrude(H)
    .edges("|Z")
    .fillet(R_OUT - T_WALL)
)
body = body.cut(cavity)

# corner bosses at ledge height
cb = CORNER_BOSS
for sx in (-1, 1):
    for sy in (-1, 1):
        x0, x1 = sorted((sx * cb, sx * (IN_HALF + 0.01)))
        y0, y1 = sorted((sy * cb, sy * (IN_HALF + 0.01)))
        blk = (
            cq.Workplane("XY")
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0)
            .extrude(Z_LEDGE)
        )
        body = body.union(blk)

# fences around the openings
body = body.union(prism(SLOT, 0, Z_SLOT_FENCE, offset=T_FENCE))
for pts in (T_OPEN, RECT_A, RECT_B):
    body = body.union(prism(pts, 0, Z_FENCE, offset=T_FENCE))

# boss
boss = (
    cq.Workplane("XY")
    .center(*BOSS_C)
    .circle(BOSS_D / 2)
    .extrude(Z_BOSS)
)
body = body.union(boss)

# pins
for (px, py, pd) in PINS:
    body = body.union(
        cq.Workplane("XY").center(px, py).circle(pd / 2).extrude(Z_PIN)
    )

# keep everything inside the outer footprint
envelope = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .rect(W, W)
    .extrude(Z_PIN + 2)
    .edges("|Z")
    .fillet(R_OUT)
)
body = body.intersect(envelope)

# openings through the floor (also trims the pin at the slot end)
for pts in (SLOT, T_OPEN, RECT_A, RECT_B):
    body = body.cut(prism(pts, -1, Z_PIN + 1))

# corner screw holes
for sx in (-1, 1):
    for sy in (-1, 1):
        hole = (
            cq.Workplane("XY")
            .workplane(offset=Z_LEDGE - CORNER_HOLE_DEPTH)
            .center(sx * CORNER_HOLE_C, sy * CORNER_HOLE_C)
            .circle(CORNER_HOLE_D / 2)
            .extrude(CORNER_HOLE_DEPTH + 1)
        )
        body = body.cut(hole)

# boss hole with countersink from below
body = body.cut(
    cq.Workplane("XY").workplane(offset=-1).center(*BOSS_C)
    .circle(BOSS_HOLE_D / 2).extrude(Z_BOSS + 2)
)
csk = cq.Solid.makeCone(
    BOSS_CSK_D / 2 + 0.6, 0.0, BOSS_CSK_D / 2 + 0.6,
    pnt=cq.Vector(BOSS_C[0], BOSS_C[1], -0.6), dir=cq.Vector(0, 0, 1)
)
body = body.cut(cq.Workplane("XY").add(csk))

# notches in the -X wall
for (y0, y1) in NOTCHES:
    n = (
        cq.Workplane("XY")
        .workplane(offset=Z_NOTCH)
        .center(-HALF - 1 + (T_WALL + 1.01) / 2, (y0 + y1) / 2)
        .rect(T_WALL + 1.01, y1 - y0)
        .extrude(H)
    )
    body = body.cut(n)

# post in the corner of the T opening (rises to pin height)
post_round = (
    cq.Workplane("XY").center(*POST_C).circle(POST_R).extrude(Z_PIN)
    .intersect(
        cq.Workplane("XY")
        .center((POST_FLAT_X - 17.0) / 2, (POST_FLAT_Y - 21.0) / 2)
        .rect(POST_FLAT_X + 17.0, POST_FLAT_Y + 21.0)
        .extrude(Z_PIN)
    )
)
tx0, tx1, ty0, ty1 = POST_TAB
post_blend = (
    prism([(tx0, ty0, 0.0), (tx1, ty0, 0.0), (tx1, ty1, 0.0), (tx0, ty1, 0.7)],
          0.0, Z_PIN)
    .cut(
        cq.Workplane("XY").workplane(offset=-1).center(*POST_COVE_C)
        .circle(POST_COVE_R).extrude(Z_PIN + 2)
    )
)
body = body.union(post_round).union(post_blend)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
